import math
import cadquery as cq
from cadquery.occ_impl.shapes import loft

# ---------------- driving dimensions (mm) ----------------
HUB_D = 11.3          # hub outer diameter
HUB_H = 9.2           # hub height (Z)
HUB_FILLET = 1.3      # round on top / bottom hub rims
BORE_D = 4.6          # shaft bore
TIP_R = 74.2          # blade tip radius (from the blade pattern centre)
BLADE_AZ = -33.5      # azimuth of blade #1 axis in the XY plane (deg)
HUB_OFFSET = 1.1      # hub axis sits this far from the blade pattern centre, toward blade #1
N_BLADES = 2
ROOT_R = HUB_OFFSET + 0.15   # blade root face: just past the hub axis for blade #1

# Blade stations, blade built along +X (local s = +Y tangential, z = Z).
# Each station: radius, leading-edge s, trailing-edge s (plan-view extents),
# leading-edge top z, trailing-edge bottom z (side-view extents), thickness.
# Leading edge sits on the -s side and high, trailing edge on +s and low.
STATIONS = [
    # r      le_s   te_s   le_z   te_z   thk
    (ROOT_R, -3.28, 5.12,  3.37, -2.96, 1.40),
    (6.0,   -3.60,  5.40,  3.50, -2.50, 1.30),
    (12.0,  -5.95,  5.40,  3.83, -1.75, 1.20),
    (20.0,  -7.85,  5.35,  3.81, -1.15, 1.05),
    (29.0,  -8.45,  5.25,  3.75, -0.52, 0.95),
    (39.0,  -7.60,  4.97,  3.52,  0.12, 0.85),
    (50.0,  -6.15,  4.45,  3.12,  0.82, 0.72),
    (61.0,  -4.60,  3.65,  2.78,  1.42, 0.58),
    (TIP_R, -2.90,  2.65,  2.52,  2.07, 0.45),
]


SECTION_PTS = 16      # samples per blade section (analytic super-ellipse)
SECTION_EXP = 2.6     # 2 = ellipse, larger = flatter plate with rounded edges
TE_TAPER = 0.6        # fraction of thickness lost toward the trailing edge


def _unit_section(t):
    """Section point for parameter t: x = -1 at the LE, +1 at the TE; unit half-thickness."""
    c, s = math.cos(t), math.sin(t)
    e = 2.0 / SECTION_EXP
    x = math.copysign(abs(c) ** e, c)
    y = math.copysign(abs(s) ** e, s) * (1.0 - TE_TAPER * ((1.0 + x) / 2.0) ** 2)
    return x, y


def _extents(a, b, beta, n=90):
    """Plan-view width and side-view height of a section of half-chord a."""
    cb, sb = math.cos(beta), math.sin(beta)
    ws, hs = [], []
    for k in range(n):
        x, y = _unit_section(2.0 * math.pi * k / n)
        ws.append(a * x * cb + b * y * sb)
        hs.append(-a * x * sb + b * y * cb)
    return max(ws) - min(ws), max(hs) - min(hs)


def _solve_section(W, Hz, b):
    """Find half-chord a and pitch beta that reproduce the measured extents."""
    a = 0.5 * math.hypot(W, Hz)
    beta = math.atan2(max(Hz - 2 * b, 0.0), W)
    for _ in range(30):
        w, h = _extents(a, b, beta)
        a += 0.5 * (W - w) * 0.8
        beta += 0.8 * (Hz - h) / max(2 * a, 1e-3)
        beta = max(0.0, beta)
    return a, beta


def station_wire(r, le_s, te_s, le_z, te_z, thk):
    """Blade section (flat super-ellipse plate) matching the station extents."""
    W = te_s - le_s                 # plan-view width
    Hz = max(le_z - te_z, thk)      # side-view height
    b = thk / 2.0
    a, beta = _solve_section(W, Hz, b)
    sc = 0.5 * (le_s + te_s)
    zc = 0.5 * (le_z + te_z)
    d = (math.cos(beta), -math.sin(beta))   # chord direction, LE -> TE
    n = (math.sin(beta), math.cos(beta))    # thickness direction
    pts = []
    for k in range(SECTION_PTS):
        x, y = _unit_section(2.0 * math.pi * k / SECTION_PTS)
        ca, sb = a * x, b * y
        pts.append(cq.Vector(r, sc + ca * d[0] + sb * n[0], zc + ca * d[1] + sb * n[1]))
    params = [float(k) for k in range(SECTION_PTS + 1)]   # identical knots on every section
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(pts, periodic=True, parameters=params)])


def make_blade():
    """Smooth cubic (chord-length parametrised) loft through the blade stations."""
    wires = [station_wire(*st) for st in STATIONS]
    return loft(wires, cap=True, ruled=False, degree=3, compat=False, parametrization="chordal")


# ---------------- hub with its shaft bore ----------------
def make_hub(seam_az):
    """Filleted cylindrical hub with a through bore; seam_az only moves the seam line."""
    body = (
        cq.Workplane("XY")
        .circle(HUB_D / 2.0)
        .extrude(HUB_H)
        .translate((0, 0, -HUB_H / 2.0))
        .edges("%CIRCLE")
        .fillet(HUB_FILLET)
    )
    bore = (
        cq.Workplane("XY")
        .circle(BORE_D / 2.0)
        .extrude(HUB_H * 2)
        .translate((0, 0, -HUB_H))
    )
    return body.cut(bore).rotate((0, 0, 0), (0, 0, 1), seam_az)


# ---------------- blades (2-fold polar pattern about an offset centre) ----------------
# The blade roots are added after the bore, so the root of blade #1 (which starts at
# the hub axis) partly closes the bore, as on the original part.
blade = make_blade()
ua = math.radians(BLADE_AZ)
pattern_centre = cq.Vector(-HUB_OFFSET * math.cos(ua), -HUB_OFFSET * math.sin(ua), 0)
blades = [
    blade.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), BLADE_AZ + i * 360.0 / N_BLADES).translate(
        pattern_centre
    )
    for i in range(N_BLADES)
]


def assemble(seam_az):
    """Fuse hub and blades; None if a boolean silently drops a blade."""
    part = make_hub(seam_az)
    for b in blades:
        before = part.val().Volume()
        part = part.union(cq.Workplane("XY").add(b))
        if part.val().Volume() - before < 0.5 * b.Volume():
            return None
    if len(part.solids().vals()) != 1 or not part.val().isValid():
        return None
    return part


# keep the hub seam on the hidden back side; try a few seam angles in case a
# boolean ever fails to fuse everything into one solid
result = None
for seam in (90.0, 130.0, 45.0, 200.0, 250.0, 300.0):
    result = assemble(seam)
    if result is not None:
        break
if result is None:  # last resort: plain union
    result = make_hub(90.0)
    for b in blades:
        result = result.union(cq.Workplane("XY").add(b))

VIEW = {"azimuth": 45, "elevation": 26}
